import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}   # default reference view

# ---------------------------------------------------------------
# Clevis bracket: vertical mounting plate (at +X) with a forged
# clevis body (block + two ears) projecting toward -X.
# Coordinates: X along the clevis (plate outer face at X=0),
# Y across the ears (symmetric), Z up (plate bottom at Z=0).
# ---------------------------------------------------------------

# ---- mounting plate ----
PLATE_T = 19.7          # thickness along X
PLATE_W = 187.5         # width along Y
PLATE_H = 143.3         # height along Z
PLATE_HOLE_D = 20.0
PLATE_HOLE_Y_NEG = -71.1
PLATE_HOLE_Y_POS = 72.65
PLATE_HOLES_NEG_Y = [23.5, 63.2]   # hole heights on the -Y side
PLATE_HOLES_POS_Y = [23.5, 68.5]   # hole heights on the +Y side

# ---- ears (clevis arms) ----
EAR_OUT = 56.1          # outer face |Y|
EAR_IN = 20.4           # inner face |Y|  (gap = 2*EAR_IN)
EYE_X, EYE_Z = -193.6, 87.4
EYE_R = 43.0
BOLT2_X, BOLT2_Z = -69.2, 44.0
HOLE_R = 10.5
TOP_SLOPE = -0.34       # upper edge of the ear (dZ/dX), tangent to the eye
LOW_SLOPE = -0.70       # lower S-curve flank (dZ/dX)
LOW_PT = (-135.5, 16.6) # a point on the lower flank
LOW_FILLET_EYE = 40.0   # concave blend eye -> lower flank
LOW_FILLET_BASE = 54.0  # convex blend lower flank -> flat bottom
EAR_EDGE_R = 7.5        # rounding of the ear perimeter edges

# ---- block (body between ears and plate) ----
BLK_X0 = -138.0         # fork-end face of the block
BLK_TOP = 147.7         # top of the block at the fork end
BLK_TOP_FILLET = 18.0   # rounding of the fork-end top edge
BLK_BOT_Z0 = 102.3      # lower edge of the block side at the fork end
BLK_BOT_Z1 = 64.05      # lower edge of the block side at the plate
BLK_HALF_W0 = 56.6      # half width at the fork end
BLK_HALF_W1 = 50.25     # half width near the plate
BLK_BOT_SINK = 1.5      # block underside sits this far inside the ears
BLK_TAPER_END = -66.0   # taper of the sides ends here
BLK_TOP_KINK_X = -71.0  # top turns from flat into the slope here

# ---- web closing the slot between the ears near the plate ----
SLOT_END_X = -30.0      # the slot between the ears ends here
SLOT_END_R = 8.0        # corner rounding of the slot end

# ---- fastener recesses ----
HEX_AF = 37.5           # hex nut pocket across flats (on -Y ear face)
HEX_DEPTH = 16.0
CB_D = 36.0             # round counterbore (on +Y ear face)
CB_DEPTH = 15.0

PX = -PLATE_T           # plate inner face (X)
X_END = -3.0            # ear / block run into the plate up to here


def blk_bot(x):
    """Z of the visible lower edge of the block side."""
    s = (BLK_BOT_Z1 - BLK_BOT_Z0) / (PX - BLK_X0)
    return BLK_BOT_Z0 + s * (x - BLK_X0)


def blk_half_w(x):
    """Half width of the block (plan view), smooth taper."""
    t = (x - BLK_X0) / (BLK_TAPER_END - BLK_X0)
    t = min(max(t, 0.0), 1.0)
    f = 0.5 * (1.0 + math.cos(math.pi * t))
    return BLK_HALF_W1 + (BLK_HALF_W0 - BLK_HALF_W1) * f


def ear_top_under_block(x):
    """Ear top edge hidden under the block, chosen so that the ear's
    rounded edge meets the (inset) block side exactly on blk_bot()."""
    r = EAR_EDGE_R
    d = EAR_OUT - blk_half_w(x)
    if d <= 0.0:
        h = r
    elif d >= r:
        h = 0.0
    else:
        h = r - math.sqrt(r * r - (r - d) ** 2)
    return blk_bot(x) + h


def top_line(x):
    """Upper tangent line of the ear (tangent to the eye circle)."""
    m = TOP_SLOPE
    return EYE_Z + EYE_R * math.sqrt(1 + m * m) + m * (x - EYE_X)


def unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


# ------------------------------------------------------------------
# Ear profile in the XZ plane
# ------------------------------------------------------------------
def ear_profile():
    m = TOP_SLOPE
    nrm = unit((-m, 1.0))           # outward normal of the top line
    T = (EYE_X + EYE_R * nrm[0], EYE_Z + EYE_R * nrm[1])

    k = LOW_SLOPE
    d_low = unit((1.0, k))          # direction along the flank (down-right)
    n_low_out = unit((k, -1.0))     # outward (material is above the line)

    # convex blend between lower flank and flat bottom (Z=0)
    xv = LOW_PT[0] - LOW_PT[1] / k
    ang = math.atan(-k)
    tl = LOW_FILLET_BASE * math.tan(ang / 2.0)
    B_flat = (xv + tl, 0.0)
    B_flank = (xv - tl * d_low[0], -tl * d_low[1])
    cB = (xv + tl, LOW_FILLET_BASE)
    midv = unit(((B_flat[0] + B_flank[0]) / 2 - cB[0],
                 (B_flat[1] + B_flank[1]) / 2 - cB[1]))
    B_mid = (cB[0] + LOW_FILLET_BASE * midv[0],
             cB[1] + LOW_FILLET_BASE * midv[1])

    # concave blend between eye circle and lower flank
    rf = LOW_FILLET_EYE
    L0 = (LOW_PT[0] + rf * n_low_out[0], LOW_PT[1] + rf * n_low_out[1])
    wx, wz = L0[0] - EYE_X, L0[1] - EYE_Z
    b = wx * d_low[0] + wz * d_low[1]
    c = wx * wx + wz * wz - (EYE_R + rf) ** 2
    t = -b + math.sqrt(b * b - c)
    cF = (L0[0] + t * d_low[0], L0[1] + t * d_low[1])
    F_flank = (cF[0] - rf * n_low_out[0], cF[1] - rf * n_low_out[1])
    ve = unit((cF[0] - EYE_X, cF[1] - EYE_Z))
    F_eye = (EYE_X + EYE_R * ve[0], EYE_Z + EYE_R * ve[1])
    midf = unit(((F_flank[0] + F_eye[0]) / 2 - cF[0],
                 (F_flank[1] + F_eye[1]) / 2 - cF[1]))
    F_mid = (cF[0] + rf * midf[0], cF[1] + rf * midf[1])

    E_mid = (EYE_X - EYE_R, EYE_Z)

    # the top line runs a little way into the block, then steps down
    # to the hidden ear edge under the block: an arc B->A tangent to a
    # straight run A->plate that is parallel to the block's lower edge
    xp = BLK_X0 + EAR_EDGE_R + 1.0
    P = (xp, top_line(xp))
    B = (xp, ear_top_under_block(xp))
    A = (BLK_TAPER_END, ear_top_under_block(BLK_TAPER_END))
    Q = (X_END, A[1] + (blk_bot(X_END) - blk_bot(A[0])))
    ln = unit((Q[0] - A[0], Q[1] - A[1]))
    nA = (-ln[1], ln[0])                      # normal pointing up
    ab = (A[0] - B[0], A[1] - B[1])
    rho = -(ab[0] ** 2 + ab[1] ** 2) / (2.0 * (nA[0] * ab[0] + nA[1] * ab[1]))
    cA = (A[0] + rho * nA[0], A[1] + rho * nA[1])
    mv = unit(((A[0] + B[0]) / 2 - cA[0], (A[1] + B[1]) / 2 - cA[1]))
    M = (cA[0] + abs(rho) * mv[0], cA[1] + abs(rho) * mv[1])

    wp = (cq.Workplane("XZ")
          .moveTo(X_END, 0.0)
          .lineTo(*B_flat)
          .threePointArc(B_mid, B_flank)
          .lineTo(*F_flank)
          .threePointArc(F_mid, F_eye)
          .threePointArc(E_mid, T)
          .lineTo(*P)
          .lineTo(*B)
          .threePointArc(M, A)
          .lineTo(*Q)
          .close())
    return wp


def make_ear(y_in, y_out):
    thick = abs(y_out - y_in)
    solid = ear_profile().extrude(thick)          # "XZ" normal is -Y
    solid = solid.translate((0, max(y_in, y_out), 0))
    solid = solid.edges("not |Y").fillet(EAR_EDGE_R)
    return solid


# ------------------------------------------------------------------
# Block: side profile (XZ) intersected with plan profile (XY)
# ------------------------------------------------------------------
def make_block():
    R = BLK_TOP_FILLET
    x_a = BLK_X0 + R
    # top: flat from the rounded fork end, bending (around BLK_TOP_KINK_X)
    # into a straight slope that meets the plate top edge
    s_top = (PLATE_H - BLK_TOP) / (PX - BLK_TOP_KINK_X)
    def slope_z(x):
        return PLATE_H + s_top * (x - PX)
    top_pts = [(BLK_TOP_KINK_X - 9.0, BLK_TOP - 0.04),
               (BLK_TOP_KINK_X + 7.0, slope_z(BLK_TOP_KINK_X + 7.0) + 0.2),
               (BLK_TOP_KINK_X + 26.0, slope_z(BLK_TOP_KINK_X + 26.0)),
               (PX, PLATE_H),
               (X_END, slope_z(X_END))]
    side = (cq.Workplane("XZ").workplane(offset=-80.0)
            .moveTo(BLK_X0, BLK_BOT_Z0 - BLK_BOT_SINK)
            .lineTo(BLK_X0, BLK_TOP - R)
            .threePointArc((BLK_X0 + R - R * math.cos(math.pi / 4),
                            BLK_TOP - R + R * math.sin(math.pi / 4)),
                           (x_a, BLK_TOP))
            .spline(top_pts, tangents=[(1.0, 0.0), (1.0, s_top)],
                    includeCurrent=True)
            .lineTo(X_END, blk_bot(X_END) - BLK_BOT_SINK)
            .lineTo(BLK_X0, BLK_BOT_Z0 - BLK_BOT_SINK)
            .close()
            .extrude(160.0))

    xs = [BLK_X0 + f * (BLK_TAPER_END - BLK_X0) for f in (0.25, 0.5, 0.75, 1.0)]
    xs += [-40.0, X_END]
    lo = [(x, -blk_half_w(x)) for x in xs]
    hi = [(x, blk_half_w(x)) for x in reversed(xs[:-1])] + \
         [(BLK_X0, BLK_HALF_W0)]
    plan = (cq.Workplane("XY")
            .moveTo(BLK_X0 - 1.0, -BLK_HALF_W0)
            .lineTo(BLK_X0, -BLK_HALF_W0)
            .spline(lo, tangents=[(1.0, 0.0), (1.0, 0.0)],
                    includeCurrent=True)
            .lineTo(X_END, BLK_HALF_W1)
            .spline(hi, tangents=[(-1.0, 0.0), (-1.0, 0.0)],
                    includeCurrent=True)
            .lineTo(BLK_X0 - 1.0, BLK_HALF_W0)
            .close()
            .extrude(BLK_TOP + 10.0))
    return side.intersect(plan)


# ------------------------------------------------------------------
# Web between the ears at the plate (the slot ends short of the plate)
# ------------------------------------------------------------------
def make_web():
    half = EAR_IN + EAR_EDGE_R          # also fills the ears' inner roundings
    x0 = SLOT_END_X - SLOT_END_R
    z_top = blk_bot(x0) + 2.0           # hidden inside the block
    web = (cq.Workplane("XY")
           .box(X_END - x0, 2 * half, z_top, centered=(False, True, False))
           .translate((x0, 0, 0)))
    slot = (cq.Workplane("XY")
            .box(60.0, 2 * EAR_IN, z_top + 20.0, centered=(False, True, False))
            .translate((SLOT_END_X - 60.0, 0, -10.0))
            .edges("|Z and >X").fillet(SLOT_END_R))
    return web.cut(slot)


# ------------------------------------------------------------------
# Plate
# ------------------------------------------------------------------
def make_plate():
    plate = (cq.Workplane("XY")
             .box(PLATE_T, PLATE_W, PLATE_H, centered=(False, True, False))
             .translate((PX, 0, 0)))
    pts = [(PLATE_HOLE_Y_NEG, z) for z in PLATE_HOLES_NEG_Y] + \
          [(PLATE_HOLE_Y_POS, z) for z in PLATE_HOLES_POS_Y]
    for (y, z) in pts:
        c = (cq.Workplane("YZ").workplane(offset=PX - 5.0)
             .center(y, z).circle(PLATE_HOLE_D / 2.0).extrude(PLATE_T + 10.0))
        plate = plate.cut(c)
    return plate


# ------------------------------------------------------------------
# Assemble
# ------------------------------------------------------------------
ear_pos = make_ear(EAR_OUT, EAR_IN)
ear_neg = ear_pos.mirror("XZ")          # identical ear on the -Y side
block = make_block()
plate = make_plate()
web = make_web()

body = plate.union(block).union(ear_neg).union(ear_pos).union(web)

for (hx, hz) in [(EYE_X, EYE_Z), (BOLT2_X, BOLT2_Z)]:
    # through hole across both ears
    hole = (cq.Workplane("XZ").workplane(offset=-80.0)
            .center(hx, hz).circle(HOLE_R).extrude(160.0))
    body = body.cut(hole)

    # hex nut pocket on the -Y face (flats horizontal)
    ac = HEX_AF / math.cos(math.pi / 6.0)   # across corners
    hex_pts = [(hx + ac / 2 * math.cos(math.radians(a)),
                hz + ac / 2 * math.sin(math.radians(a)))
               for a in range(0, 360, 60)]
    hexcut = (cq.Workplane("XZ").workplane(offset=EAR_OUT - HEX_DEPTH)
              .polyline(hex_pts).close().extrude(HEX_DEPTH + 10.0))
    body = body.cut(hexcut)

    # round counterbore (bolt head) on the +Y face
    cb = (cq.Workplane("XZ").workplane(offset=-(EAR_OUT + 10.0))
          .center(hx, hz).circle(CB_D / 2.0).extrude(CB_DEPTH + 10.0))
    body = body.cut(cb)

result = body
